"""Bullet-shaped plug with an elliptical cross-section.

Axis along X.  Cross-section is an ellipse, twice as tall (Z) as it is thick (Y).
  * rear end  (-X): half spheroid dome, tangent to the body
  * body          : straight elliptical cylinder
  * front end (+X): pointed elliptical cone, sharp edge where it meets the body
"""
import math

import cadquery as cq
from cadquery.occ_impl.shapes import loft
from OCP.gp import gp_Elips, gp_Ax2, gp_Pnt, gp_Dir
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# ---------------- driving dimensions (mm) ----------------
SEMI_Y = 10.0          # half thickness of the elliptical section (Y)
SEMI_Z = 20.0          # half height of the elliptical section (Z)
BODY_LEN = 20.0        # straight elliptical-cylinder length along X
CONE_LEN = 10.0        # length of the pointed elliptical cone at +X
# the rear dome is a half spheroid whose depth along X equals SEMI_Y
# (round in the top view, half-elliptical in the side view)
DOME_LEN = SEMI_Y


def section(x0):
    """Elliptical cross-section face (SEMI_Y x SEMI_Z) in the plane x = x0.

    The closed ellipse edge is parametrised to start on the +Y (back) side so
    the seam of the faces swept from it lies on the back of the part."""
    ax = gp_Ax2(gp_Pnt(x0, 0, 0), gp_Dir(1, 0, 0), gp_Dir(0, 0, 1))
    ell = gp_Elips(ax, SEMI_Z, SEMI_Y)          # major axis along Z
    u0 = -math.pi / 2                           # -> point (x0, +SEMI_Y, 0)
    edge = cq.Edge(BRepBuilderAPI_MakeEdge(ell, u0, u0 + 2 * math.pi).Edge())
    return cq.Face.makeFromWires(cq.Wire.assembleEdges([edge]))


# ---------------- straight elliptical body (x = 0 .. BODY_LEN) ----------------
body = cq.Workplane("XY").add(
    cq.Solid.extrudeLinear(section(0.0), cq.Vector(BODY_LEN, 0, 0))
)

# ---------------- rounded rear end: half spheroid on x <= 0 ----------------
# half-ellipse profile (radial semi-axis DOME_LEN, height semi-axis SEMI_Z) on
# the +Y side of the YZ plane, revolved 180 deg about the Z axis so that it
# sweeps through the -X half space and closes onto the body's rear face
dome = (
    cq.Workplane("YZ")
    .moveTo(0, -SEMI_Z)
    .ellipseArc(DOME_LEN, SEMI_Z, angle1=-90, angle2=90, startAtCurrent=True)
    .close()
    .revolve(180, (0, 0, 0), (0, 1, 0))
)

# ---------------- pointed elliptical cone on the front face ----------------
# ruled loft from the front elliptical section to the apex on the X axis
cone_apex = cq.Vertex.makeVertex(BODY_LEN + CONE_LEN, 0, 0)
cone = cq.Workplane("XY").add(loft([section(BODY_LEN), cone_apex], ruled=True))

result = body.union(dome).union(cone).clean().solids()

VIEW = {"azimuth": 45, "elevation": 26}
